import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
R_OUT = 50.0          # outer radius of the cup
H = 62.0              # overall height
T_WALL = 1.75         # wall thickness
T_FLOOR = 2.0         # floor thickness
CH_OUT = 4.8          # 45 deg chamfer at the outer bottom edge
CH_IN = 2.8           # 45 deg chamfer at the inner floor/wall junction

# vent slots (48 positions, some left solid)
N_SLOT = 48
SLOT_OFFSET = 3.75    # deg, angle of first slot position
SLOT_W = 3.0          # regular slot width
SLOT_W_NARROW = 1.55  # slots flanking the 0/90/180/270 deg webs
SLOT_W_CHAN = 2.3     # slots through the channel bulge
SLOT_Z0 = 7.5
SLOT_Z1 = 57.5
CHAN_RECESS_Z1 = 61.6  # shallow recess continues the channel slots up to just below the rim
CHAN_RECESS_D = 1.0
SKIP_SLOTS = [41.25, 138.75, 168.75, 176.25, 183.75, 191.25, 221.25, 318.75]

# vertical wire channel (groove outside / bulge inside)
CHAN_ANG = 120.0
CHAN_D = 49.5         # distance of channel axis from cup axis
CHAN_R = 6.6          # groove radius

# standoffs
SO_X = 32.6
SO_Y = 27.2
SO_D = 9.2
SO_TOP = 35.9
SO_TOP_CH = 0.8
SO_HOLE = 2.9
SO_CB_D = 4.8
SO_CB_DEPTH = 1.2
SO_CB_CH = 0.6
SO_BOT_CSK = 6.0

# centre (shaft) hole
HOLE_X = 14.0
HOLE_D = 14.4

# small boss + inner rib at -X
PIN_X = -32.5
PIN_D = 6.4
PIN_TOP = 7.7
RIB_T = 1.2
RIB_TOP_Z = 45.8
RIB_END_X = -35.3   # where the sloped rib edge lands on the small boss
SMALL_HOLE = 2.0
SMALL_CSK = 4.4

# mounting tab at -X
TAB_END_R = 8.0
TAB_CX = -60.0
TAB_T = 7.4
TAB_POCKET = 3.5
TAB_WALL = 1.6
TAB_BOSS_D = 6.8
GUSSET_TOP_Z = 46.0
GUSSET_X0 = -60.5
GUSSET_FOOT_R = 1.0


def cyl(r, h, x=0.0, y=0.0, z=0.0):
    return cq.Workplane("XY").workplane(offset=z).center(x, y).circle(r).extrude(h)


def cone(r0, r1, h, x=0.0, y=0.0, z=0.0):
    """frustum from radius r0 at z to radius r1 at z+h"""
    return cq.Workplane("XY").add(
        cq.Solid.makeCone(r0, r1, h, cq.Vector(x, y, z), cq.Vector(0, 0, 1)))


# ---------------- cup body ----------------
outer = cyl(R_OUT, H).faces("<Z").edges().chamfer(CH_OUT)

cavity = (cyl(R_OUT - T_WALL, H + 1, z=T_FLOOR)
          .faces("<Z").edges().chamfer(CH_IN))

cax = CHAN_D * math.cos(math.radians(CHAN_ANG))
cay = CHAN_D * math.sin(math.radians(CHAN_ANG))
bulge = cyl(CHAN_R + T_WALL, H + 4, cax, cay, -1)
cavity = cavity.cut(bulge)

# ---------------- mounting tab (outside, fills under the chamfer) ----------------
tab_x0 = -(R_OUT - CH_OUT - 1.0)
tab = (cq.Workplane("XY")
       .moveTo(tab_x0, -TAB_END_R)
       .lineTo(TAB_CX, -TAB_END_R)
       .threePointArc((TAB_CX - TAB_END_R, 0), (TAB_CX, TAB_END_R))
       .lineTo(tab_x0, TAB_END_R)
       .close()
       .extrude(TAB_T))
ri = TAB_END_R - TAB_WALL
pocket = (cq.Workplane("XY").workplane(offset=TAB_T - TAB_POCKET)
          .moveTo(-R_OUT + 1.0, -ri)
          .lineTo(TAB_CX, -ri)
          .threePointArc((TAB_CX - ri, 0), (TAB_CX, ri))
          .lineTo(-R_OUT + 1.0, ri)
          .close()
          .extrude(TAB_POCKET + 1))
pocket = pocket.cut(cyl(R_OUT, H))
tab = tab.cut(pocket)
tab = tab.union(cyl(TAB_BOSS_D / 2, TAB_T, TAB_CX, 0, 0))

# gusset ribs along both tab edges, tying the tab to the wall
for sy in (1, -1):
    yc = sy * (TAB_END_R - TAB_WALL / 2)
    g = (cq.Workplane("XZ", origin=(0, yc, 0))
         .polyline([(GUSSET_X0, TAB_T - 0.5), (-R_OUT + 1.0, GUSSET_TOP_Z),
                    (-R_OUT + 1.0, TAB_T - 0.5)])
         .close()
         .extrude(TAB_WALL / 2, both=True))
    tab = tab.union(g)

# small round where the sloped gusset edge runs into the top of the tab
x_foot = GUSSET_X0 + 0.5 * (-R_OUT + 1.0 - GUSSET_X0) / (GUSSET_TOP_Z - TAB_T + 0.5)


class _RibFoot(cq.Selector):
    def filter(self, objs):
        out = []
        for e in objs:
            if e.geomType() != "LINE":
                continue
            a, b = e.startPoint(), e.endPoint()
            if (abs(a.x - b.x) < 1e-3 and abs(a.z - b.z) < 1e-3 and abs(a.x - x_foot) < 0.05
                    and abs(a.z - TAB_T) < 0.05 and abs(a.y - b.y) > 0.5):
                out.append(e)
        return out


try:
    tab = tab.edges(_RibFoot()).fillet(GUSSET_FOOT_R)
except Exception:
    pass

body = outer.union(tab).cut(cavity)

groove = cyl(CHAN_R, H + 4, cax, cay, -1)
body = body.cut(groove)

# ---------------- standoffs ----------------
so_pts = [(sx * SO_X, sy * SO_Y) for sx in (1, -1) for sy in (1, -1)]
for (x, y) in so_pts:
    post = (cyl(SO_D / 2, SO_TOP - 1.0, x, y, 1.0)
            .faces(">Z").edges().chamfer(SO_TOP_CH))
    body = body.union(post)

# ---------------- small boss and inner rib ----------------
body = body.union(cyl(PIN_D / 2, PIN_TOP - 1.0, PIN_X, 0, 1.0))

x_wall = -(R_OUT - T_WALL) - 0.5
rib = (cq.Workplane("XZ")
       .polyline([(x_wall, 1.0), (x_wall, RIB_TOP_Z), (x_wall + 2.2, RIB_TOP_Z),
                  (RIB_END_X, PIN_TOP - 0.2), (RIB_END_X, 1.0)])
       .close()
       .extrude(RIB_T / 2, both=True))
body = body.union(rib)

# ---------------- vent slots ----------------
cardinals = [0.0, 90.0, 180.0, 270.0, 360.0]
for k in range(N_SLOT):
    ang = SLOT_OFFSET + k * 360.0 / N_SLOT
    if any(abs(ang - s) < 0.5 for s in SKIP_SLOTS):
        continue
    near_chan = abs(ang - CHAN_ANG) < 8.0
    r0 = 38.0 if near_chan else R_OUT - T_WALL - 2.0
    r1 = R_OUT + 2.0
    z1 = SLOT_Z1
    # narrow slots next to the wide cardinal webs
    w = SLOT_W_CHAN if near_chan else SLOT_W
    yoff = 0.0
    for c in cardinals:
        d = ang - c
        if abs(d) < 4.0:
            w = SLOT_W_NARROW
            yoff = math.copysign((SLOT_W - SLOT_W_NARROW) / 2, d)
    cutter = (cq.Workplane("XY")
              .box(r1 - r0, w, z1 - SLOT_Z0, centered=(False, True, False))
              .translate((r0, yoff, SLOT_Z0))
              .rotate((0, 0, 0), (0, 0, 1), ang))
    body = body.cut(cutter)
    if near_chan:
        # shallow recess on the inner face of the channel bulge, up to the rim
        strip = (cq.Workplane("XY")
                 .box(r1 - r0, w, CHAN_RECESS_Z1 - z1 + 0.2, centered=(False, True, False))
                 .translate((r0, yoff, z1 - 0.1))
                 .rotate((0, 0, 0), (0, 0, 1), ang))
        shell = (cyl(CHAN_R + T_WALL + 1.0, H + 4, cax, cay, -1)
                 .cut(cyl(CHAN_R + T_WALL - CHAN_RECESS_D, H + 4, cax, cay, -1)))
        body = body.cut(strip.intersect(shell))

# ---------------- holes ----------------
body = body.cut(cyl(HOLE_D / 2, 10, HOLE_X, 0, -1))
for (x, y) in so_pts:
    body = body.cut(cyl(SO_HOLE / 2, SO_TOP + 2, x, y, -1))
    # counterbore with chamfered entry at the top of the standoff
    body = body.cut(cyl(SO_CB_D / 2, SO_CB_DEPTH + 1, x, y, SO_TOP - SO_CB_DEPTH))
    body = body.cut(cone(SO_CB_D / 2, SO_CB_D / 2 + SO_CB_CH + 0.5, SO_CB_CH + 0.5,
                         x, y, SO_TOP - SO_CB_CH))
    # countersink from below
    body = body.cut(cone(SO_BOT_CSK / 2 + 0.5, 0.0, SO_BOT_CSK / 2 + 0.5, x, y, -0.5))

# small blind holes from below (boss and tab boss)
for (x, y) in [(PIN_X, 0.0), (TAB_CX, 0.0)]:
    body = body.cut(cyl(SMALL_HOLE / 2, 4.5, x, y, -1))
    body = body.cut(cone(SMALL_CSK / 2 + 0.5, 0.0, SMALL_CSK / 2 + 0.5, x, y, -0.5))

result = body

VIEW = {"azimuth": 45, "elevation": 26}
